import math
import cadquery as cq

# ---------------------------------------------------------------
# Double-ended hose-barb reducer with a mounting flange.
# Axis of revolution = Y.  Large barb end at the -Y side (y = 0),
# small barb end at +Y.  Profiles are drawn as (radius, axial) in
# the XY plane and revolved about the Y axis.
# (In the reference, the small-side spigot sits very slightly
#  eccentric to the flange axis - SMALL_OFFSET_X.)
# ---------------------------------------------------------------

# --- large barb end ---
LB_N = 3              # number of large barbs
LB_LEN = 8.92         # axial length of one large barb
LB_ROOT_R = 6.04      # barb root radius (tip side of each barb)
LB_CREST_R = 8.56     # barb crest radius (sharp, before rounding)
LB_TIP_RND = 1.8      # rounding of the large hose-end lip
LB_CREST_RND = 1.3    # rounding of each barb crest

# --- transition cone + body ---
CONE_START_R = 6.36
CONE_LEN = 8.88
BODY_R = 10.64
BODY_LEN = 17.88

# --- flange + collar ---
FLANGE_R = 16.68
FLANGE_T = 3.92
COLLAR_R = 11.2
COLLAR_T = 1.6

# --- small side ---
SCYL_R = 7.06
SCYL_LEN = 11.68
SCONE_END_R = 4.0
SCONE_LEN = 6.2
SB_N = 3
SB_LEN = 6.0
SB_CREST_R = 5.85
SB_ROOT_R = 4.02
SB_TIP_RND = 1.3
SB_CREST_RND = 1.0
SMALL_OFFSET_X = 0.32  # eccentricity of collar / small spigot / small bore

# --- bore ---
BORE_R = 2.9          # through bore (small side)
LBORE_R = 4.44        # enlarged bore in the large barb end
LBORE_DEPTH = 26.0    # depth of enlarged bore from the large end
BORE_STEP_LEN = 1.9   # axial length of the bore transition
BORE_STEP_RND = 4.0   # rounding of the transition

SEAM_ROT = 110.0      # turn the cosmetic revolve seam to the underside


def filleted_profile(wp, verts):
    """Closed polygon of (x, y, r) vertices; r > 0 rounds that corner
    with a tangent arc.  Returns a closed wire on the workplane."""
    n = len(verts)
    segs = []
    for i in range(n):
        px, py, rad = verts[i]
        if rad <= 0:
            segs.append(((px, py), None, (px, py)))
            continue
        ax, ay, _ = verts[i - 1]
        bx, by, _ = verts[(i + 1) % n]
        u1 = (ax - px, ay - py)
        u2 = (bx - px, by - py)
        l1 = math.hypot(*u1)
        l2 = math.hypot(*u2)
        u1 = (u1[0] / l1, u1[1] / l1)
        u2 = (u2[0] / l2, u2[1] / l2)
        cth = max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1]))
        th = math.acos(cth)
        t = rad / math.tan(th / 2.0)
        d = rad / math.sin(th / 2.0)
        bx_, by_ = u1[0] + u2[0], u1[1] + u2[1]
        bl = math.hypot(bx_, by_)
        bx_, by_ = bx_ / bl, by_ / bl
        t1 = (px + u1[0] * t, py + u1[1] * t)
        t2 = (px + u2[0] * t, py + u2[1] * t)
        mid = (px + bx_ * (d - rad), py + by_ * (d - rad))
        segs.append((t1, mid, t2))
    w = wp.moveTo(*segs[0][2])
    for i in list(range(1, n)) + [0]:
        t1, mid, t2 = segs[i]
        w = w.lineTo(*t1)
        if mid is not None:
            w = w.threePointArc(mid, t2)
    return w.close()


def revolve_y(verts, dx=0.0):
    """Revolve a (radius, axial, rounding) profile about the Y axis,
    turn the seam away, and shift it sideways by dx."""
    s = filleted_profile(cq.Workplane("XY"), verts).revolve(
        360, (0, 0, 0), (0, 1, 0))
    s = s.rotate((0, 0, 0), (0, 1, 0), SEAM_ROT)
    if dx:
        s = s.translate((dx, 0, 0))
    return s


# ---------------- large side + flange (on main axis) ----------------
VA = [(0.0, 0.0, 0.0), (LB_ROOT_R, 0.0, LB_TIP_RND)]
for i in range(LB_N):
    y1 = (i + 1) * LB_LEN
    VA.append((LB_CREST_R, y1, LB_CREST_RND))     # barb crest
    nxt = LB_ROOT_R if i < LB_N - 1 else CONE_START_R
    VA.append((nxt, y1, 0.0))                     # barb root / cone start
y = LB_N * LB_LEN + CONE_LEN
VA.append((BODY_R, y, 0.0))
y += BODY_LEN
Y_FLANGE0 = y
VA.append((BODY_R, y, 0.0))
VA.append((FLANGE_R, y, 0.0))
y += FLANGE_T
Y_FLANGE1 = y
VA.append((FLANGE_R, y, 0.0))
VA.append((0.0, y, 0.0))
large_side = revolve_y(VA)

# ---------------- collar + small spigot (slightly eccentric) --------
y = Y_FLANGE1 - 1.0
VB = [(0.0, y, 0.0), (COLLAR_R, y, 0.0)]
y = Y_FLANGE1 + COLLAR_T
VB.append((COLLAR_R, y, 0.0))
VB.append((SCYL_R, y, 0.0))
y += SCYL_LEN
VB.append((SCYL_R, y, 0.0))
y += SCONE_LEN
VB.append((SCONE_END_R, y, 0.0))
for i in range(SB_N):
    VB.append((SB_CREST_R, y, SB_CREST_RND))      # small barb crest
    y += SB_LEN
    last = i == SB_N - 1
    VB.append((SB_ROOT_R, y, SB_TIP_RND if last else 0.0))
Y_END = y
VB.append((0.0, Y_END, 0.0))
small_side = revolve_y(VB, SMALL_OFFSET_X)

body = large_side.union(small_side)

# ---------------- bores ----------------
# enlarged entry bore, concentric with the flange
VC = [
    (0.0, -1.0, 0.0),
    (LBORE_R, -1.0, 0.0),
    (LBORE_R, LBORE_DEPTH + 0.3, 0.0),
    (0.0, LBORE_DEPTH + 0.3, 0.0),
]
large_bore = revolve_y(VC)

# rounded transition + through bore, concentric with the small spigot
y_t = LBORE_DEPTH + BORE_STEP_LEN
VD = [
    (0.0, LBORE_DEPTH, 0.0),
    (LBORE_R + SMALL_OFFSET_X, LBORE_DEPTH, 0.0),
    (BORE_R, y_t, BORE_STEP_RND),
    (BORE_R, Y_END + 1.0, 0.0),
    (0.0, Y_END + 1.0, 0.0),
]
small_bore = revolve_y(VD, SMALL_OFFSET_X)

body = body.cut(large_bore).cut(small_bore)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
